import cadquery as cq
import math

# ---------------------------------------------------------------
# Housing with dovetail rail -- all dimensions derived from a
# reference unit grid (U) and converted to millimetres.
# ---------------------------------------------------------------
U = 0.25  # mm per reference unit

# --- main body --------------------------------------------------
BODY_L = 195 * U          # body length (x) up to top rail chamfer start
BODY_W = 150 * U          # body width (y)
BODY_H = 60 * U           # body height (z)
CORNER_R = 18 * U         # vertical corner radius at -X end
TAPER_X = 177.5 * U       # x where side faces start to taper in
TAPER_END_X = 196 * U     # x where the taper reaches the rail width
RAIL_HW = 68.5 * U        # half width of the rail (y)

TOP_FILLET = 2.2 * U
BOT_FILLET = 1.4 * U
RIM_FILLET = 2.5 * U

# --- rail profile (x, z) ---------------------------------------
NECK_END_X = 225 * U
FLARE_END_X = 231.5 * U
HEAD_END_X = 236 * U
HEAD_TOP = 51.25 * U
HEAD_BOT = 16.25 * U
NECK_TOP = 46.5 * U
NECK_BOT = 20.2 * U
BOT_STEP_X = 197 * U      # small vertical step under the rail root
BOT_STEP_Z = 8.5 * U
GROOVE_R = 3.0 * U
HEAD_ROUND = 1.5 * U
END_CHAMFER = 2.0 * U

# --- cavities ---------------------------------------------------
SHELF_Z = 46 * U          # upper recess floor
UP_X0, UP_X1 = 9.7 * U, 177.7 * U
UP_HW = 65.4 * U
UP_R = 8.5 * U

FLOOR_Z = 10.5 * U        # deepest floor
STEP_Z = 16.5 * U         # raised floor steps
XA_X0, XA_X1 = 13.5 * U, 173.3 * U
XA_HW = 29.75 * U
YA_X0, YA_X1 = 53.9 * U, 141.5 * U
YA_Y0, YA_Y1 = -61.6 * U, 60.2 * U
BOSS_R = 17 * U
STEP_Y = -(XA_HW + BOSS_R)  # step line in the -Y arm (end of boss round)
BOSS_CHAMFER = 2.0 * U
BASE_FILLET = 2.5 * U

# --- holes --------------------------------------------------------
HOLE_XS = (35.2 * U, 159.1 * U)
HOLE_Y = 48.1 * U
CB_D = 19.4 * U
CB_DEPTH = 4.7 * U
HOLE_D = 13.8 * U

# --- windows ----------------------------------------------------
WIN_W = 24.5 * U          # along y
WIN_Z0, WIN_Z1 = 15.4 * U, 40.8 * U
SLOT_X = 98 * U
SLOT_L = 54.5 * U
SLOT_H = 29 * U
SLOT_Z = FLOOR_Z + SLOT_H / 2   # slot sill flush with the floor

# --- small D tab -------------------------------------------------
TAB_X0, TAB_X1 = 44.6 * U, 51.2 * U
TAB_YC = -0.6 * U
TAB_HW = 5.5 * U
TAB_FLAT = 1.7 * U        # straight part of the tab sides
TAB_TIP = 2.0 * U         # size of the rounded tip
TAB_TOP = 33 * U

EPS = 1e-3


def pick_edges(wp, pred):
    """Return a workplane holding the edges of wp satisfying pred(edge)."""
    es = [e for e in wp.edges().vals() if pred(e)]
    return wp.newObject(es)


def bb(e):
    return e.BoundingBox()


# ================================================================
# body outline (XY): straight sides, rounded -X corners, sides
# tapering in towards the rail and continuing past the rail root
TAPER_SLOPE = (BODY_W / 2 - RAIL_HW) / (TAPER_END_X - TAPER_X)
XFAR = 216 * U
yfar = BODY_W / 2 - (XFAR - TAPER_X) * TAPER_SLOPE
body_xy = (
    cq.Workplane("XY")
    .polyline([
        (0, -BODY_W / 2),
        (TAPER_X, -BODY_W / 2),
        (XFAR, -yfar),
        (XFAR, yfar),
        (TAPER_X, BODY_W / 2),
        (0, BODY_W / 2),
    ])
    .close()
    .extrude(BODY_H)
    .edges("|Z and <X")
    .fillet(CORNER_R)
)

# body side profile (XZ): 45 deg chamfers down to the rail neck with
# concave rounds forming the dovetail groove
c45 = math.sqrt(0.5)
gd = GROOVE_R * math.tan(math.radians(22.5))   # tangent setback
top_corner = (BODY_L + (BODY_H - NECK_TOP), NECK_TOP)
bot_corner = (BOT_STEP_X + (NECK_BOT - BOT_STEP_Z), NECK_BOT)


def groove_arc(corner, up):
    """Concave round between a 45 deg chamfer and the neck face."""
    s = 1 if up else -1
    cx, cz = corner
    t_ch = (cx - gd * c45, cz + s * gd * c45)      # on the chamfer
    t_nk = (cx + gd, cz)                           # on the neck face
    cen = (cx + gd, cz + s * GROOVE_R)
    a = math.radians(-90 - 22.5) if up else math.radians(90 + 22.5)
    mid = (cen[0] + GROOVE_R * math.cos(a), cen[1] + GROOVE_R * math.sin(a))
    return t_ch, mid, t_nk


top_ch, top_mid, top_nk = groove_arc(top_corner, True)
bot_ch, bot_mid, bot_nk = groove_arc(bot_corner, False)
NECK_IN = XFAR - 2 * U

body_xz = (
    cq.Workplane("XZ")
    .moveTo(-1, -1)
    .lineTo(BOT_STEP_X, -1)
    .lineTo(BOT_STEP_X, BOT_STEP_Z)
    .lineTo(*bot_ch)
    .threePointArc(bot_mid, bot_nk)
    .lineTo(NECK_IN, NECK_BOT)
    .lineTo(NECK_IN, NECK_TOP)
    .lineTo(*top_nk)
    .threePointArc(top_mid, top_ch)
    .lineTo(BODY_L, BODY_H)
    .lineTo(BODY_L, BODY_H + 1)
    .lineTo(-1, BODY_H + 1)
    .close()
    .extrude(BODY_W, both=True)
)
body = body_xy.intersect(body_xz)

# rail neck + dovetail head, running the full rail length
rail_pts = [
    (TAPER_END_X - 6 * U, NECK_BOT),
    (NECK_END_X, NECK_BOT),
    (FLARE_END_X, HEAD_BOT),
    (HEAD_END_X, HEAD_BOT),
    (HEAD_END_X, HEAD_TOP),
    (FLARE_END_X, HEAD_TOP),
    (NECK_END_X, NECK_TOP),
    (TAPER_END_X - 6 * U, NECK_TOP),
]
rail = (
    cq.Workplane("XZ")
    .polyline(rail_pts)
    .close()
    .extrude(RAIL_HW, both=True)
)
# chamfer the outline of both rail end faces (root edge is buried)
rail = pick_edges(
    rail,
    lambda e: bb(e).ylen < EPS and abs(abs(bb(e).ymin) - RAIL_HW) < EPS
    and bb(e).xmax > TAPER_END_X,
).chamfer(END_CHAMFER)
# round the four long edges of the rail head
rail = pick_edges(
    rail,
    lambda e: bb(e).ylen > 2 * RAIL_HW - 4 * END_CHAMFER
    and bb(e).xlen < EPS
    and (abs(bb(e).xmin - HEAD_END_X) < EPS
         or abs(bb(e).xmin - FLARE_END_X) < EPS),
).fillet(HEAD_ROUND)
body = body.union(rail, clean=True)

# soft outer top edge and bottom edge of the body
body = pick_edges(
    body,
    lambda e: abs(bb(e).zmin - BODY_H) < EPS and bb(e).zlen < EPS
    and bb(e).xmin < BODY_L - 1 * U,
).fillet(TOP_FILLET)
body = pick_edges(
    body,
    lambda e: abs(bb(e).zmax) < EPS and bb(e).zlen < EPS
    and bb(e).xmax < TAPER_X + EPS,
).fillet(BOT_FILLET)

# ---------------------------------------------------------------
# upper recess
upper = (
    cq.Workplane("XY")
    .workplane(offset=SHELF_Z)
    .center((UP_X0 + UP_X1) / 2, 0)
    .rect(UP_X1 - UP_X0, 2 * UP_HW)
    .extrude(BODY_H)
    .edges("|Z")
    .fillet(UP_R)
)
body = body.cut(upper)
body = pick_edges(
    body,
    lambda e: abs(bb(e).zmin - BODY_H) < EPS and bb(e).zlen < EPS
    and bb(e).xmin > UP_X0 - EPS and bb(e).xmax < UP_X1 + EPS
    and bb(e).ymin > -UP_HW - EPS and bb(e).ymax < UP_HW + EPS,
).fillet(RIM_FILLET)


def plus_tool(x_arm, y_arm, z0, z1, corners):
    """Plus shaped prism, rounding the re-entrant corners listed and the
    bottom outline (gives concave rounds at the pocket floor)."""
    (ax0, ax1, ahw) = x_arm
    (bx0, bx1, by0, by1) = y_arm
    a = cq.Workplane("XY").workplane(offset=z0).center((ax0 + ax1) / 2, 0)\
        .rect(ax1 - ax0, 2 * ahw).extrude(z1 - z0)
    b = cq.Workplane("XY").workplane(offset=z0)\
        .center((bx0 + bx1) / 2, (by0 + by1) / 2)\
        .rect(bx1 - bx0, by1 - by0).extrude(z1 - z0)
    t = a.union(b, clean=True)
    chosen = []
    for e in t.edges("|Z").vals():
        c = e.Center()
        for (cx, cy) in corners:
            if abs(c.x - cx) < EPS and abs(c.y - cy) < EPS:
                chosen.append(e)
    if chosen:
        t = t.newObject(chosen).fillet(BOSS_R)
    # round only the boss walls at the floor, not the arm end walls
    ends_x = (ax0, ax1)
    ends_y = (by0, by1)

    def boss_base(e):
        b = bb(e)
        if b.xlen < EPS and any(abs(b.xmin - v) < EPS for v in ends_x):
            return False
        if b.ylen < EPS and any(abs(b.ymin - v) < EPS for v in ends_y):
            return False
        return True

    es = [e for e in t.faces("<Z").edges().vals() if boss_base(e)]
    t = t.newObject(es).fillet(BASE_FILLET)
    return t


# cross shaped pocket: arms end on raised floor steps
cross = plus_tool(
    (XA_X0, XA_X1, XA_HW),
    (YA_X0, YA_X1, YA_Y0, YA_Y1),
    STEP_Z, SHELF_Z + 0.01,
    [(YA_X0, XA_HW), (YA_X0, -XA_HW), (YA_X1, XA_HW), (YA_X1, -XA_HW)],
)
# deeper central part of the pocket (full height so walls stay clean)
_c = math.sqrt(0.5)
_bx = YA_X0 - BOSS_R
deep = (
    cq.Workplane("XY").workplane(offset=FLOOR_Z)
    .moveTo(XA_X0, -XA_HW)
    .lineTo(_bx, -XA_HW)
    .threePointArc((_bx + BOSS_R * _c, -XA_HW - BOSS_R + BOSS_R * _c), (YA_X0, STEP_Y))
    .lineTo(YA_X1, STEP_Y)
    .lineTo(YA_X1, YA_Y1)
    .lineTo(YA_X0, YA_Y1)
    .lineTo(YA_X0, XA_HW + BOSS_R)
    .threePointArc((_bx + BOSS_R * _c, XA_HW + BOSS_R - BOSS_R * _c), (_bx, XA_HW))
    .lineTo(XA_X0, XA_HW)
    .close()
    .extrude(SHELF_Z + 0.01 - FLOOR_Z)
)


def _deep_boss_base(e):
    b = bb(e)
    if abs(b.zmax - FLOOR_Z) > EPS:
        return False
    if b.xlen < EPS and (abs(b.xmin - XA_X0) < EPS or abs(b.xmin - YA_X1) < EPS):
        return False
    if b.ylen < EPS and (abs(b.ymin - STEP_Y) < EPS or abs(b.ymin - YA_Y1) < EPS):
        return False
    return True


deep = deep.newObject([e for e in deep.edges().vals() if _deep_boss_base(e)])\
    .fillet(BASE_FILLET)
body = body.cut(cross.union(deep))

# chamfer the top edges of the corner bosses (pocket rim at shelf level)
body = pick_edges(
    body,
    lambda e: abs(bb(e).zmin - SHELF_Z) < EPS and bb(e).zlen < EPS
    and bb(e).xmin > XA_X0 - EPS and bb(e).xmax < XA_X1 + EPS
    and bb(e).ymin > YA_Y0 - EPS and bb(e).ymax < YA_Y1 + EPS,
).chamfer(BOSS_CHAMFER)

# ---------------------------------------------------------------
# counterbored holes in the four corner bosses
hole_pts = [(x, s * HOLE_Y) for x in HOLE_XS for s in (1, -1)]
cb_tool = (
    cq.Workplane("XY").workplane(offset=SHELF_Z - CB_DEPTH)
    .pushPoints(hole_pts).circle(CB_D / 2).extrude(CB_DEPTH + 1)
)
thru_tool = (
    cq.Workplane("XY").workplane(offset=-1)
    .pushPoints(hole_pts).circle(HOLE_D / 2).extrude(SHELF_Z + 2)
)
body = body.cut(cb_tool).cut(thru_tool)

# rectangular window through the -X wall
win = (
    cq.Workplane("YZ")
    .workplane(offset=-1)
    .center(0, (WIN_Z0 + WIN_Z1) / 2)
    .rect(WIN_W, WIN_Z1 - WIN_Z0)
    .extrude(XA_X0 + 2)
)
body = body.cut(win)

# obround slot through the +Y wall
slot = (
    cq.Workplane("XZ")
    .workplane(offset=-(BODY_W / 2 + 1))
    .center(SLOT_X, SLOT_Z)
    .slot2D(SLOT_L, SLOT_H)
    .extrude(BODY_W / 2 - YA_Y1 + 2)
)
body = body.cut(slot)

# small bullet shaped locating tab standing on the floor
tab = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR_Z - 0.01)
    .center(0, TAB_YC)
    .moveTo(TAB_X0, -TAB_HW)
    .lineTo(TAB_X0 + TAB_FLAT, -TAB_HW)
    .lineTo(TAB_X1 - TAB_TIP, -TAB_TIP * 1.4)
    .threePointArc((TAB_X1, 0), (TAB_X1 - TAB_TIP, TAB_TIP * 1.4))
    .lineTo(TAB_X0 + TAB_FLAT, TAB_HW)
    .lineTo(TAB_X0, TAB_HW)
    .close()
    .extrude(TAB_TOP - FLOOR_Z)
)
body = body.union(tab)

result = body
